import math
import cadquery as cq

# Threaded retaining ring: plain cylindrical outside, flat top and bottom faces,
# internal single-start right-hand trapezoidal (60 deg, ISO-like) thread running
# out through both faces, with a 45 deg lead-in chamfer at the top of the bore.

# ---------------- driving dimensions (mm) ----------------
OD = 100.0            # outer diameter
H = 29.7              # ring height
R_OUT = OD / 2.0
R_CHAMFER_TOP = 45.3  # radius where the 45 deg entry chamfer meets the top face
CHAMFER_ANGLE = 45.0  # chamfer angle from the axis

PITCH = 11.7          # thread pitch (single start, right hand)
R_MAJOR = 45.0        # thread root radius (major diameter, just inside the chamfer)
FLANK_ANGLE = 30.0    # flank angle from the radial plane (60 deg included)
CREST = PITCH / 4.0   # crest flat width (at the minor radius)
ROOT = PITCH / 8.0    # root flat width (at the major radius)
DEPTH = (PITCH / 2.0 - (CREST + ROOT) / 2.0) / math.tan(math.radians(FLANK_ANGLE))
R_MINOR = R_MAJOR - DEPTH   # thread crest radius (bore radius)
# thread phase: the centre of a crest lies at this height at polar angle 135 deg
CREST_Z_AT_135 = 19.45

# polar angles at which the (purely cosmetic) seam lines of the revolved faces lie
OUTER_SEAM_DEG = 90.0
INNER_SEAM_DEG = 270.0

VIEW = {"azimuth": 45, "elevation": 26}

# ---------------- base blank (solid; bore is cut after the thread) ----------------
blank = cq.Solid.makeCylinder(R_OUT, H).rotate(
    cq.Vector(0, 0, 0), cq.Vector(0, 0, 1), OUTER_SEAM_DEG
)
ring = cq.Workplane("XY").add(blank)

# ---------------- helical thread groove ----------------
tan_f = math.tan(math.radians(FLANK_ANGLE))
# groove centre height at polar angle 0 (right-hand: z rises with the polar angle)
groove_z0 = CREST_Z_AT_135 - PITCH * 135.0 / 360.0 + PITCH / 2.0
# start the helix a little more than one pitch below the part, end above it
n_below = math.ceil((groove_z0 + PITCH) / PITCH)
z_start = groove_z0 - n_below * PITCH
helix_height = (H + 2.0 * PITCH) - z_start

helix = cq.Wire.makeHelix(
    pitch=PITCH,
    height=helix_height,
    radius=R_MINOR,
    center=cq.Vector(0, 0, z_start),
    dir=cq.Vector(0, 0, 1),
)


def thread_groove(ext):
    """Trapezoidal groove profile in the XZ plane swept along the helix.
    `ext` lets the profile reach a little inside the bore for a clean cut."""
    half_root = ROOT / 2.0
    half_open = half_root + (DEPTH + ext) * tan_f
    pts = [
        (R_MINOR - ext, z_start - half_open),
        (R_MAJOR, z_start - half_root),
        (R_MAJOR, z_start + half_root),
        (R_MINOR - ext, z_start + half_open),
    ]
    return (
        cq.Workplane("XZ")
        .polyline(pts)
        .close()
        .sweep(cq.Workplane().add(helix), isFrenet=True)
    )


v_blank = blank.Volume()
threaded = None
for ext in (1.0, 1.3, 0.7):
    cand = ring.cut(thread_groove(ext))
    if cand.val().isValid() and cand.val().Volume() < v_blank - 1.0:
        threaded = cand
        break
ring = threaded if threaded is not None else ring

# ---------------- bore (thread crest / minor diameter) ----------------
bore = cq.Solid.makeCylinder(R_MINOR, H + 2.0, cq.Vector(0, 0, -1.0)).rotate(
    cq.Vector(0, 0, 0), cq.Vector(0, 0, 1), INNER_SEAM_DEG
)
ring = ring.cut(cq.Workplane("XY").add(bore))

# ---------------- 45 deg entry chamfer at the top of the bore ----------------
drop = 12.0
run = drop * math.tan(math.radians(CHAMFER_ANGLE))
chamfer_cut = (
    cq.Workplane("XZ")
    .polyline(
        [
            (0, H - drop),
            (R_CHAMFER_TOP - run, H - drop),
            (R_CHAMFER_TOP + 1.0 * math.tan(math.radians(CHAMFER_ANGLE)), H + 1.0),
            (0, H + 1.0),
        ]
    )
    .close()
    .revolve(360, (0, 0, 0), (0, 1, 0))
    .rotate((0, 0, 0), (0, 0, 1), INNER_SEAM_DEG)
)
ring = ring.cut(chamfer_cut)

result = ring
